import cadquery as cq

# ---------------------------------------------------------------
# Stepped sleeve: Ø50 tube ending in a Ø45.6 spigot (cup) at the
# bottom. The cup floor has a large inner fillet and a ring of
# 12 through holes.
# ---------------------------------------------------------------

# Driving dimensions (mm)
R_UP = 25.0        # upper tube outer radius
R_UP_IN = 22.7     # upper tube bore radius
R_LO = 22.8        # spigot (lower cup) outer radius
R_LO_IN = 21.4     # cup bore radius
H_TOTAL = 108.5    # overall height
H_LO = 34.5        # exposed length of the spigot (external step height)
Z_CUP_TOP = 40.0   # internal shoulder where the cup bore meets the tube bore
T_FLOOR = 6.5      # floor thickness at the centre
R_FIL = 10.0       # fillet between cup bore and floor
N_HOLES = 12
PCD_R = 17.0       # pitch-circle radius of the holes
HOLE_D = 7.8

# cosmetic only: angular position of the cylinder seams (kept out of sight)
SEAM_OUT = 180.0   # outer cylinders
SEAM_BORE = 225.0  # upper bore
SEAM_CAV = 180.0   # cup cavity (seam runs under a hole)


def turned(wp, ang):
    return wp.rotate((0, 0, 0), (0, 0, 1), ang)


def cyl(r, z0, z1, ang):
    return turned(cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0), ang)


# outer envelope: spigot + main tube
body = cyl(R_LO, 0.0, H_LO, SEAM_OUT).union(cyl(R_UP, H_LO, H_TOTAL, SEAM_OUT))

# upper bore from the top down to the internal shoulder
body = body.cut(cyl(R_UP_IN, Z_CUP_TOP, H_TOTAL + 1.0, SEAM_BORE))

# cup cavity with a large fillet into the floor
cavity = (cq.Workplane("XY").workplane(offset=T_FLOOR)
          .circle(R_LO_IN).extrude(Z_CUP_TOP + 1.0 - T_FLOOR)
          .edges("<Z").fillet(R_FIL))
body = body.cut(turned(cavity, SEAM_CAV))

# ring of through holes in the floor (one on each 30-degree axis)
holes = (cq.Workplane("XY").polarArray(PCD_R, 0, 360, N_HOLES)
         .circle(HOLE_D / 2).extrude(T_FLOOR + R_FIL + 2.0)
         .translate((0, 0, -1.0)))
result = body.cut(holes)

VIEW = {"azimuth": 45, "elevation": 26}
